import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm).  X = width, Y = length (front face at
# Y=0, the print-bed face), Z = height (bottom of the arc at Z=0)
# ---------------------------------------------------------------
L = 76.0            # overall length of the base sector (Y)
R_ARC = 38.8        # radius of the cylindrical base
ZC_ARC = 38.8       # Z of the base-arc centre
LEG_ANG = 30.0      # legs lean 30 deg from vertical
T_LEG = 6.6         # leg / wall thickness
CX, CZ = 15.95, 26.9  # leg-outer / shoulder corner (right side)
WALL_OUT_Z = 75.2   # Z of the outer top corner of the side walls
PLATE_TOP = 62.6    # motor plate top surface
PLATE_T = 5.0       # motor plate thickness
CAV_BOT = 30.1      # bottom of the central triangular cavity
CAV_R = 5.0         # cavity corner radius
WALL_FILLET = 4.3   # fillet wall-inner-face / plate

EAR_R = 10.1        # anti-warp "mouse ear" discs on the front face
EAR_X, EAR_Z = 36.8, 70.3
EAR_T = 1.3

CH = 20.3           # square channel for a 2020 extrusion
CH_Z = 14.75
TAB_W, TAB_D = 5.5, 1.9
TAB_D_BOT = 0.8
CH_R = 0.35

BACK_Y0, BACK_Z0, BACK_K = 59.2, 75.4, 0.36   # tilted back: Y = Y0 + K(Z0-Z)
WALL_TOP_R = 3.0

WEB_Y0, WEB_Y1 = 33.5, 35.5   # central web splitting the cavity

MOTOR_Y = 30.0
MOTOR_HOLE = 24.1
MOTOR_DEPTH = 4.0    # blind recess for the motor boss
MOTOR_PITCH = 31.0
MOTOR_SCREW = 3.2

GROOVE_Y = (10.0, 50.0)
GROOVE_W = 5.0
GROOVE_D = 1.0
GROOVE_START = 0.5   # grooves stop just short of the shoulder
PAD_H = 0.45         # raised pad between the grooves
PAD_TOP_Z = 68.0     # pad ends at the upper cross holes
WALL_HOLE_D = 5.5    # cross holes through the legs (perpendicular)
WALL_HOLE_Z = (68.3, 36.5)

HEX_X, HEX_Z = 22.15, 19.05   # nut pockets in the base sector
HEX_AF = 11.7
HEX_DRAFT = 26.0               # pointed (printable) pocket ends
FRONT_HEX_DEPTH = 2.9
BACK_HEX_Y = 57.0
TRAP_Y0, TRAP_Y1 = 26.2, 33.8  # central drop-in nut trap
TRAP_SWEEP = 3.6
TRAP_TAPER_L = 5.8
TRAP_DRAFT = 43.0

BOT_HOLE_Y = (15.0, 45.0)     # small vertical holes into the cavity
CB_HOLE_Y = (19.5, 49.5)      # counterbored bolts into the 2020 slot
CB_HOLE_D, CB_D, CB_DEPTH = 5.3, 10.0, 1.8
SMALL_HOLE_X, SMALL_HOLE_D = 16.0, 2.8

tan = math.tan(math.radians(LEG_ANG))
sin = math.sin(math.radians(LEG_ANG))
cos = math.cos(math.radians(LEG_ANG))
dx_leg = T_LEG / cos                       # horizontal leg thickness


def x_outer(z):
    return CX + (z - CZ) * tan


def x_inner(z):
    return CX - dx_leg + (z - CZ) * tan


# ---------------------------------------------------------------
# main profile in the XZ plane
# ---------------------------------------------------------------
# shoulder line meets the base circle
a = 1.0
b = 2 * (CX * cos - (CZ - ZC_ARC) * sin)
c = CX ** 2 + (CZ - ZC_ARC) ** 2 - R_ARC ** 2
t = (-b + math.sqrt(b * b - 4 * a * c)) / 2
AX, AZ = CX + cos * t, CZ - sin * t

D = (x_outer(WALL_OUT_Z), WALL_OUT_Z)
E = (D[0] - T_LEG * cos, D[1] + T_LEG * sin)
F = (x_inner(PLATE_TOP), PLATE_TOP)

pts_right = [(AX, AZ), (CX, CZ), D, E, F]
pts_left = [(-p[0], p[1]) for p in reversed(pts_right)]

prof = (
    cq.Workplane("XZ")
    .moveTo(-AX, AZ)
    .threePointArc((0, ZC_ARC - R_ARC), (AX, AZ))
)
for p in pts_right[1:]:
    prof = prof.lineTo(*p)
for p in pts_left[:-1]:
    prof = prof.lineTo(*p)
body = prof.close().extrude(-L)


# concave fillets between side walls and the motor plate
body = body.edges(
    cq.selectors.BoxSelector((F[0] - 0.5, -1, F[1] - 0.5), (F[0] + 0.5, L + 1, F[1] + 0.5))
).fillet(WALL_FILLET)
body = body.edges(
    cq.selectors.BoxSelector((-F[0] - 0.5, -1, F[1] - 0.5), (-F[0] + 0.5, L + 1, F[1] + 0.5))
).fillet(WALL_FILLET)

# ---------------------------------------------------------------
# tilted back face of the upper frame
# ---------------------------------------------------------------
n = cq.Vector(0, 1, BACK_K).normalized()
back_cut = cq.Workplane(
    cq.Plane(origin=(0, BACK_Y0 + BACK_K * BACK_Z0, 0), xDir=(1, 0, 0), normal=n.toTuple())
).rect(400, 400).extrude(200)
body = body.cut(back_cut)

# round the top/back corner of the side walls
for sx in (-1, 1):
    xc = sx * (D[0] + E[0]) / 2
    zc = (D[1] + E[1]) / 2
    yc = BACK_Y0 + BACK_K * (BACK_Z0 - zc)
    body = body.edges(
        cq.selectors.BoxSelector((xc - 3.5, yc - 2.5, zc - 2.5), (xc + 3.5, yc + 2.5, zc + 2.5))
    ).fillet(WALL_TOP_R)

# ---------------------------------------------------------------
# mouse-ear discs on the front face
# ---------------------------------------------------------------
for sx in (-1, 1):
    ear = cq.Workplane("XZ").center(sx * EAR_X, EAR_Z).circle(EAR_R).extrude(-EAR_T)
    body = body.union(ear)

# ---------------------------------------------------------------
# central triangular cavity (front and back pockets, web between)
# ---------------------------------------------------------------
cav_top = PLATE_TOP - PLATE_T
cav_pts = [
    (-x_inner(CAV_BOT), CAV_BOT),
    (x_inner(CAV_BOT), CAV_BOT),
    (x_inner(cav_top), cav_top),
    (-x_inner(cav_top), cav_top),
]


def cavity(y0, y1):
    s = cq.Workplane("XZ", origin=(0, y0, 0)).polyline(cav_pts).close().extrude(-(y1 - y0))
    return s.edges("|Y").fillet(CAV_R)


body = body.cut(cavity(-1, WEB_Y0)).cut(cavity(WEB_Y1, L + 5))

# ---------------------------------------------------------------
# square channel for the 2020 extrusion (through, with key tabs)
# ---------------------------------------------------------------
h = CH / 2
tw = TAB_W / 2
tb = TAB_D_BOT
ch_pts = [
    (-h, -h), (-tw, -h), (-tw, -h + tb), (tw, -h + tb), (tw, -h),
    (h, -h), (h, -tw), (h - TAB_D, -tw), (h - TAB_D, tw), (h, tw),
    (h, h), (tw, h), (tw, h - TAB_D), (-tw, h - TAB_D), (-tw, h),
    (-h, h), (-h, tw), (-h + TAB_D, tw), (-h + TAB_D, -tw), (-h, -tw),
]
ch_pts = [(p[0], p[1] + CH_Z) for p in ch_pts]
channel = (
    cq.Workplane("XZ", origin=(0, -1, 0))
    .polyline(ch_pts)
    .close()
    .extrude(-(L + 2))
    .edges("|Y")
    .fillet(CH_R)
)
body = body.cut(channel)

# ---------------------------------------------------------------
# motor plate holes (NEMA17 pattern)
# ---------------------------------------------------------------
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, PLATE_TOP - MOTOR_DEPTH))
    .center(0, MOTOR_Y)
    .circle(MOTOR_HOLE / 2)
    .extrude(50)
)
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.cut(
            cq.Workplane("XY", origin=(0, 0, PLATE_TOP - PLATE_T - 0.5))
            .center(sx * MOTOR_PITCH / 2, MOTOR_Y + sy * MOTOR_PITCH / 2)
            .circle(MOTOR_SCREW / 2)
            .extrude(PLATE_T + 1)
        )

# ---------------------------------------------------------------
# grooves and cross holes in the leg outer faces
# ---------------------------------------------------------------
leg_len = 70.0
# slightly raised pad on each leg between the two grooves
pad_len = (PAD_TOP_Z - CZ) / cos
for sx in (-1, 1):
    pad = (
        cq.Workplane("XY")
        .box(PAD_H + 0.5, GROOVE_Y[1] - GROOVE_Y[0], pad_len, centered=(False, True, False))
        .translate((-0.5, (GROOVE_Y[0] + GROOVE_Y[1]) / 2, 0))
        .rotate((0, 0, 0), (0, 1, 0), LEG_ANG)
        .translate((CX, 0, CZ))
    )
    if sx < 0:
        pad = pad.mirror("YZ")
    body = body.union(pad)

for sx in (-1, 1):
    for gy in GROOVE_Y:
        g = (
            cq.Workplane("XY")
            .box(2 * GROOVE_D, GROOVE_W, leg_len, centered=(True, True, False))
            .translate((0, 0, GROOVE_START))
            .rotate((0, 0, 0), (0, 1, 0), LEG_ANG)
            .translate((CX, gy, CZ))
        )
        if sx < 0:
            g = g.mirror("YZ")
        body = body.cut(g)
        for hz in WALL_HOLE_Z:
            xm = x_outer(hz) - dx_leg / 2
            hole = (
                cq.Workplane("XY")
                .circle(WALL_HOLE_D / 2)
                .extrude(30, both=True)
                .rotate((0, 0, 0), (0, 1, 0), 90 + LEG_ANG)
                .translate((xm, gy, hz))
            )
            if sx < 0:
                hole = hole.mirror("YZ")
            body = body.cut(hole)

# ---------------------------------------------------------------
# hex nut pockets (front, back, and a central drop-in trap)
# ---------------------------------------------------------------
hex_d = HEX_AF / math.cos(math.radians(30))
apex = (HEX_AF / 2) / math.tan(math.radians(HEX_DRAFT)) - 0.2


def hex_prism(y0, y1):
    return (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .center(HEX_X, HEX_Z)
        .polygon(6, hex_d)
        .extrude(-(y1 - y0))
    )


def hex_point(y0, direction):
    wp = cq.Workplane("XZ", origin=(0, y0, 0)).center(HEX_X, HEX_Z).polygon(6, hex_d)
    return wp.extrude(-direction * apex, taper=HEX_DRAFT)


# the central nut trap is a hexagon swept up towards the leg/shoulder
# corner so that a nut can be dropped in from the side
hr = hex_d / 2
sx_, sz_ = -0.5 * TRAP_SWEEP, 0.866 * TRAP_SWEEP
hv = [(hr * math.cos(math.radians(ang)), hr * math.sin(math.radians(ang))) for ang in range(0, 360, 60)]
trap_pts = [
    hv[0],
    (hv[1][0] + sx_, hv[1][1] + sz_),
    (hv[2][0] + sx_, hv[2][1] + sz_),
    (hv[3][0] + sx_, hv[3][1] + sz_),
    hv[4],
    hv[5],
]
trap_pts = [(HEX_X + p[0], HEX_Z + p[1]) for p in trap_pts]


def trap_part(y0, y1=None, direction=0):
    wp = cq.Workplane("XZ", origin=(0, y0, 0)).polyline(trap_pts).close()
    if y1 is not None:
        return wp.extrude(-(y1 - y0))
    return wp.extrude(-direction * TRAP_TAPER_L, taper=TRAP_DRAFT)


pockets = [
    hex_prism(-1, FRONT_HEX_DEPTH).union(hex_point(FRONT_HEX_DEPTH, 1)),
    hex_prism(BACK_HEX_Y, L + 1).union(hex_point(BACK_HEX_Y, -1)),
    trap_part(TRAP_Y0, TRAP_Y1)
    .union(trap_part(TRAP_Y1, direction=1))
    .union(trap_part(TRAP_Y0, direction=-1)),
]
for p in pockets:
    body = body.cut(p).cut(p.mirror("YZ"))

# ---------------------------------------------------------------
# bottom holes: counterbored bolts into the channel, small pilot holes
# ---------------------------------------------------------------
for by in CB_HOLE_Y:
    body = body.cut(
        cq.Workplane("XY", origin=(0, 0, -1)).center(0, by).circle(CB_HOLE_D / 2).extrude(12)
    )
    body = body.cut(
        cq.Workplane("XY", origin=(0, 0, -1)).center(0, by).circle(CB_D / 2).extrude(1 + CB_DEPTH)
    )
for by in BOT_HOLE_Y:
    for sx in (-1, 1):
        body = body.cut(
            cq.Workplane("XY", origin=(0, 0, -1))
            .center(sx * SMALL_HOLE_X, by)
            .circle(SMALL_HOLE_D / 2)
            .extrude(45)
        )

result = body

VIEW = {"azimuth": 45, "elevation": 26}
